import cadquery as cq

# ============ driving dimensions (mm) ============
# Enclosure front cover: stands upright, width along X, height along Z,
# front (closed) face at y = 0, open back (rim) at y = T.
W = 60.0          # width  (X)
H = 100.0         # height (Z)
T = 11.3          # depth  (Y)
R_CORNER = 3.0    # radius of the four Y-parallel outer corners
R_FRONT = 3.0     # round-over of the front face perimeter
WALL = 1.6        # side wall thickness
FLOOR = 1.8       # front plate thickness
R_INNER = 2.0     # inside fillet, front plate to walls
BOSS = 8.2        # corner screw boss size, measured from the outer faces
R_BOSS = 2.0      # radius on the boss corners inside the cavity
SCREW_D = 2.4     # corner screw hole diameter
SCREW_OFF = 3.9   # screw hole centre offset from the outer faces
SCREW_DEPTH = 7.0 # blind depth of the screw holes from the rim

# ---- front features (x, z from part centre, seen from the front) ----
HOLE_D = 10.0
HOLE_X, HOLE_Z = -18.7, 35.5
WIN_X, WIN_Z = 0.0, 35.5
WIN_W, WIN_H = 18.6, 10.3        # through window
WIN_RW, WIN_RH = 20.6, 12.0      # shallow recess framing the window
WIN_RD = 1.2                     # recess depth
SIDE_SLOT = (3.6, 6.8)           # w x h, snap slots near the side walls
SIDE_SLOT_X, SIDE_SLOT_Z = 23.9, -4.25
BOT_SLOT = (7.0, 3.7)            # w x h, snap slots near the bottom wall
BOT_SLOT_X, BOT_SLOT_Z = 15.1, -44.0

# ---- PCB standoffs on the inside of the front plate ----
# (x, z, outer dia, hole dia)
STANDOFF_H = 2.2
STANDOFF_FIL = 0.5
STANDOFFS = [(8.7, 24.9, 3.0, 1.6), (-9.7, 24.8, 3.0, 1.6),
             (9.3, 1.6, 3.8, 2.0), (-10.3, 1.5, 3.8, 2.0),
             (13.0, -28.8, 3.8, 2.0), (-13.9, -28.9, 3.8, 2.0)]


def xz(x, y, z):
    """Workplane parallel to XZ through (x, y, z); its normal is -Y."""
    return cq.Workplane("XZ", origin=(x, y, z))


# ============ outer body ============
outer = xz(0, 0, 0).rect(W, H).extrude(-T)          # y: 0 -> T
outer = outer.edges("|Y").fillet(R_CORNER)
outer = outer.faces("<Y").edges().fillet(R_FRONT)

# ============ cavity (open to +Y) ============
iw, ih = W - 2 * WALL, H - 2 * WALL
cav = xz(0, FLOOR, 0).rect(iw, ih).extrude(-T)
bs = BOSS - WALL
corner_blocks = (xz(0, 0, 0)
                 .rarray(iw - bs, ih - bs, 2, 2)
                 .rect(bs, bs).extrude(-(T + 2)))
cav = cav.cut(corner_blocks)
cav = cav.edges("|Y").fillet(R_BOSS)
cav = cav.faces("<Y").edges().fillet(R_INNER)

body = outer.cut(cav)

# corner screw holes (blind, from the rim)
screws = (xz(0, T + 0.5, 0)
          .rarray(W - 2 * SCREW_OFF, H - 2 * SCREW_OFF, 2, 2)
          .circle(SCREW_D / 2).extrude(SCREW_DEPTH + 0.5))
body = body.cut(screws)

# ============ standoffs (revolved, with a small root fillet) ============
for (x, z, d, dh) in STANDOFFS:
    ro, rh, f = d / 2, dh / 2, STANDOFF_FIL
    prof = (cq.Workplane("XY")
            .moveTo(rh, -0.3)
            .lineTo(ro + f, -0.3)
            .lineTo(ro + f, 0)
            .radiusArc((ro, f), f)
            .lineTo(ro, STANDOFF_H)
            .lineTo(rh, STANDOFF_H)
            .close()
            .revolve(360, (0, 0, 0), (0, 1, 0)))
    body = body.union(prof.translate((x, FLOOR, z)))

# ============ front openings ============
hole = xz(HOLE_X, -1, HOLE_Z).circle(HOLE_D / 2).extrude(-(FLOOR + 2))
rec = xz(WIN_X, -1, WIN_Z).rect(WIN_RW, WIN_RH).extrude(-(1 + WIN_RD))
win = xz(WIN_X, -1, WIN_Z).rect(WIN_W, WIN_H).extrude(-(FLOOR + 2))
body = body.cut(hole).cut(rec).cut(win)

side_slots = (xz(0, -1, SIDE_SLOT_Z).rarray(2 * SIDE_SLOT_X, 1, 2, 1)
              .rect(*SIDE_SLOT).extrude(-(FLOOR + 4)))
bot_slots = (xz(0, -1, BOT_SLOT_Z).rarray(2 * BOT_SLOT_X, 1, 2, 1)
             .rect(*BOT_SLOT).extrude(-(FLOOR + 4)))
body = body.cut(side_slots).cut(bot_slots)

result = body
VIEW = {"azimuth": 45, "elevation": 26}
